import cadquery as cq
import math
from OCP.gp import gp_GTrsf
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform

# ---------------------------------------------------------------------------
# Exploded "BOB BOT" enclosure: housing, front panel, gasket frame, lid, tray
# All dimensions in millimetres.
# ---------------------------------------------------------------------------

# ---- housing (box) --------------------------------------------------------
BOX_W = 49.5          # X
BOX_D = 53.0          # Y (front face at Y=0, open back at Y=BOX_D)
BOX_H = 82.2          # Z
WALL = 1.8
BOX_R = 2.6           # outer edge rounding
IN_R = 1.5            # inner edge rounding of the shells
BACK_R = 1.0          # rounding of the rim round the open back

# ---- underside details of the housing ---------------------------------------
NOTCH_W, NOTCH_H = 4.2, 0.7        # step along the rear bottom edge
FOOT_Y, FOOT_W, FOOT_H = 37.5, 1.2, 0.45   # small rib under the floor

# ---- front-face features (shared by housing and loose front panel) --------
RING_Z = 57.7         # ring centre height
RING_R = 21.7         # ring outer radius
HOLE_R = 14.1         # through hole radius
BOSS_T = 4.3          # boss protrusion
STEM_HW = 16.2        # half width of the stem under the ring
STEM_Z0 = 32.0        # bottom of the stem
KEY_RC = 5.0          # concave blend between ring and stem
KEY_RB = 2.4          # stem corner radius
BOSS_FILLET = 2.0     # 3D rounding of the boss outer edge
HOLE_FILLET = 0.4     # 3D rounding of the hole edge
TUBE_R = 18.0         # outer radius of the lens tube behind the ring
TUBE_TOP = 4.2        # tube end, measured from the outer face into the part

WIN = 10.5            # square windows
WIN_PITCH = 13.8
WIN_Z0 = 20.3

OPEN_X0, OPEN_X1 = 24.0, 45.6     # lower-right opening
OPEN_Z0, OPEN_Z1 = 1.9, 19.1
CUT_R = 0.5           # corner radius of windows and opening

TEXT_H = 1.0          # emboss height of lettering
TEXT_SIZE = 6.4
TEXT_STRETCH = 1.25               # lettering is a wide face
TEXT_X = (4.4, 12.0, 19.7)        # letter centres
TEXT_Z = (11.2, 7.0)              # baselines of the two lines
TEXT_LINES = ("BOB", "BOT")
FONT_PATH = "/usr/share/fonts/truetype/dejavu/DejaVuSerif-Bold.ttf"

# ---- side port on the housing (-X face) -----------------------------------
PORT_Y, PORT_Z = 33.6, 43.6
PORT_L, PORT_H, PORT_T = 8.4, 4.6, 0.6
PORT_SLOT_L, PORT_SLOT_H = 6.0, 2.4

# ---- inner shelf and rails --------------------------------------------------
SHELF_Z = 39.8
SHELF_T = 1.2
SHELF_Y0 = 19.0
RAIL_W, RAIL_H = 1.0, 1.0
SHELF_RAIL_Y = (23.0, 44.0)
FLOOR_RAIL_Y = (23.0, 44.0)

# ---- loose front panel ----------------------------------------------------
PANEL_D = 8.55
PANEL_FRONT_R = 2.4
PANEL_POS = (-42.95, -12.3, 0.0)

# ---- gasket frame ---------------------------------------------------------
FR_W, FR_H, FR_D = 49.8, 82.2, 5.55
FR_BAR = 1.6          # bar width of the frame
FR_R = 2.6            # corner radius
FR_FRONT_R = 1.5      # rounding of the outer front edge (bar looks like a rod)
FR_LIP = 0.6          # inner lip on the back half
FR_LIP_D = 2.2
FR_POS = (-58.35, -48.1, 0.9)      # centre X, centre Y, bottom Z

# ---- lid ------------------------------------------------------------------
LID_W, LID_H, LID_T = 48.75, 81.0, 1.5
LID_EDGE_R = 0.6
LID_SQ = 18.0
LID_SQ_Z = 18.2
LID_POS = (-62.3, -67.8, 0.4)

# ---- tray -----------------------------------------------------------------
TR_L = 49.5
TR_W = 31.8
TR_BASE_W = 28.0
TR_BASE_T = 1.0
TR_BASE_Z = 1.7       # underside of the tray floor above the tray bottom
TR_PLATE_T = 2.0
TR_PLATE_H = 12.7
TR_WIN_W, TR_WIN_Z0, TR_WIN_Z1 = 8.6, 2.3, 7.3
TR_STOP_T = 1.9
TR_STOP_H = 3.8
TR_SLOT_W = 3.6
TR_SLOT_Y = 9.9
TR_SLOT_GAP = 3.4
TR_POS = (-7.95, -55.35, 1.5)      # min X, centre Y, bottom Z


def xz_plane(y):
    """Plane parallel to XZ at height Y=y, local x=X, local y=Z, normal -Y."""
    return cq.Workplane(cq.Plane(origin=(0, y, 0), xDir=(1, 0, 0), normal=(0, -1, 0)))


def keyhole(y_start, length, cx, cz, R, hw, z0, rc, rb):
    """Ring with a stem underneath (keyhole outline) extruded from Y=y_start
    towards -Y.  rc: concave blend ring/stem, rb: stem corner radius."""
    zf = cz - math.sqrt((R + rc) ** 2 - (hw + rc) ** 2)
    tx = R * (hw + rc) / (R + rc)
    tz = cz + R * (zf - cz) / (R + rc)
    a0 = math.pi
    a1 = math.atan2(tz - zf, cx + tx - (cx + hw + rc))
    am = 0.5 * (a0 + a1)
    mcx, mcz = cx + hw + rc + rc * math.cos(am), zf + rc * math.sin(am)
    s45 = math.sqrt(0.5)
    w = (xz_plane(y_start)
         .moveTo(cx, z0)
         .lineTo(cx + hw - rb, z0)
         .threePointArc((cx + hw - rb + rb * s45, z0 + rb - rb * s45), (cx + hw, z0 + rb))
         .lineTo(cx + hw, zf)
         .threePointArc((mcx, mcz), (cx + tx, tz))
         .threePointArc((cx, cz + R), (cx - tx, tz))
         .threePointArc((2 * cx - mcx, mcz), (cx - hw, zf))
         .lineTo(cx - hw, z0 + rb)
         .threePointArc((cx - hw + rb - rb * s45, z0 + rb - rb * s45), (cx - hw + rb, z0))
         .close())
    return w.extrude(length)


def y_box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def letter(ch):
    """One embossed letter, centred on X=0, baseline Z=0, rising towards -Y."""
    t = xz_plane(0).text(ch, TEXT_SIZE, TEXT_H + 0.3, font="DejaVu Serif",
                         kind="bold", fontPath=FONT_PATH, halign="center",
                         valign="bottom")
    g = gp_GTrsf()
    g.SetValue(1, 1, TEXT_STRETCH)
    sh = cq.Shape.cast(BRepBuilderAPI_GTransform(t.val().wrapped, g, True).Shape())
    return cq.Workplane("XY").add(sh)


def front_features(body, W, H):
    """Add ring boss, windows, opening and lettering to a wall whose outer
    face is Y=0 (facing -Y) and whose inner face is Y=WALL."""
    cx = W / 2.0
    # boss
    boss = keyhole(0.6, BOSS_T + 0.6, cx, RING_Z, RING_R, STEM_HW, STEM_Z0,
                   KEY_RC, KEY_RB)
    boss = boss.faces("<Y").edges().fillet(BOSS_FILLET)
    bhole = (xz_plane(1.0).center(cx, RING_Z).circle(HOLE_R).extrude(BOSS_T + 2))
    boss = boss.cut(bhole)
    sel = cq.selectors.BoxSelector((cx - 1, -BOSS_T - 0.5, RING_Z - 1),
                                   (cx + 1, -BOSS_T + 0.5, RING_Z + 1))
    boss = boss.edges(sel).fillet(HOLE_FILLET)
    body = body.union(boss)
    # hollow the boss from the inside, leaving a lens tube round the hole
    # that stands proud of the inner face of the wall
    inner = keyhole(WALL + 0.01, BOSS_T + 0.01, cx, RING_Z, RING_R - WALL,
                    STEM_HW - WALL, STEM_Z0 + WALL, KEY_RC + WALL, max(KEY_RB - WALL, 0.5))
    tube = (xz_plane(TUBE_TOP).center(cx, RING_Z).circle(TUBE_R)
            .extrude(TUBE_TOP + BOSS_T - WALL + 0.2))
    body = body.cut(inner.cut(tube)).union(tube)
    # through hole
    hole = (xz_plane(TUBE_TOP + 1).center(cx, RING_Z).circle(HOLE_R)
            .extrude(TUBE_TOP + BOSS_T + 3))
    body = body.cut(hole)
    # three square windows
    wins = (cq.Workplane("XZ", origin=(0, WALL + 1, 0))
            .pushPoints([(cx + i * WIN_PITCH, WIN_Z0 + WIN / 2.0) for i in (-1, 0, 1)])
            .rect(WIN, WIN).extrude(WALL + 3).edges("|Y").fillet(CUT_R))
    body = body.cut(wins)
    # lower opening
    opening = (cq.Workplane("XZ", origin=(0, WALL + 1, 0))
               .center((OPEN_X0 + OPEN_X1) / 2.0, (OPEN_Z0 + OPEN_Z1) / 2.0)
               .rect(OPEN_X1 - OPEN_X0, OPEN_Z1 - OPEN_Z0).extrude(WALL + 3)
               .edges("|Y").fillet(CUT_R))
    body = body.cut(opening)
    # lettering
    try:
        letters = None
        for line, zb in zip(TEXT_LINES, TEXT_Z):
            for ch, xc in zip(line, TEXT_X):
                t = letter(ch).translate((xc, 0.3, zb))
                letters = t if letters is None else letters.union(t)
        body = body.union(letters)
    except Exception:
        pass
    return body


# ---------------------------------------------------------------------------
# housing
# ---------------------------------------------------------------------------
def make_box():
    outer = (cq.Workplane("XY").box(BOX_W, BOX_D, BOX_H, centered=False)
             .edges("not >Y").fillet(BOX_R)
             .faces(">Y").edges().fillet(BACK_R))
    cav = y_box(WALL, BOX_W - WALL, WALL, BOX_D + 1, WALL, BOX_H - WALL)
    cav = cav.edges("not >Y").fillet(IN_R)
    body = outer.cut(cav)
    # rabbet round the open back
    rab = y_box(WALL * 0.5, BOX_W - WALL * 0.5, BOX_D - 1.5, BOX_D + 1,
                WALL * 0.5, BOX_H - WALL * 0.5).edges("|Y").fillet(BOX_R - WALL * 0.5)
    body = body.cut(rab)
    # step along the rear bottom edge and a small rib under the floor
    body = body.cut(y_box(-1, BOX_W + 1, BOX_D - NOTCH_W, BOX_D + 1, -1, NOTCH_H))
    body = body.union(y_box(BOX_R, BOX_W - BOX_R, FOOT_Y - FOOT_W / 2,
                            FOOT_Y + FOOT_W / 2, -FOOT_H, 0.5))
    body = front_features(body, BOX_W, BOX_H)
    # shelf with two rails, two rails on the floor
    shelf = y_box(WALL - 0.1, BOX_W - WALL + 0.1, SHELF_Y0, BOX_D - 1.5,
                  SHELF_Z, SHELF_Z + SHELF_T)
    for yr in SHELF_RAIL_Y:
        shelf = shelf.union(y_box(WALL - 0.1, BOX_W - WALL + 0.1, yr - RAIL_W / 2,
                                  yr + RAIL_W / 2, SHELF_Z + SHELF_T,
                                  SHELF_Z + SHELF_T + RAIL_H))
    for yr in FLOOR_RAIL_Y:
        shelf = shelf.union(y_box(WALL - 0.1, BOX_W - WALL + 0.1, yr - RAIL_W / 2,
                                  yr + RAIL_W / 2, WALL - 0.1, WALL + RAIL_H))
    body = body.union(shelf)
    # side port: small raised frame with a slot on the -X face
    port = y_box(-PORT_T, 0.5, PORT_Y - PORT_L / 2, PORT_Y + PORT_L / 2,
                 PORT_Z - PORT_H / 2, PORT_Z + PORT_H / 2)
    body = body.union(port)
    slot = y_box(-PORT_T - 1, WALL + 1, PORT_Y - PORT_SLOT_L / 2, PORT_Y + PORT_SLOT_L / 2,
                 PORT_Z - PORT_SLOT_H / 2, PORT_Z + PORT_SLOT_H / 2)
    body = body.cut(slot)
    return body


def make_panel():
    outer = (cq.Workplane("XY").box(BOX_W, PANEL_D, BOX_H, centered=False)
             .edges("|Y").fillet(BOX_R)
             .faces("<Y").edges().fillet(PANEL_FRONT_R))
    cav = y_box(WALL, BOX_W - WALL, WALL, PANEL_D + 1, WALL, BOX_H - WALL)
    cav = cav.edges("not >Y").fillet(IN_R)
    body = outer.cut(cav)
    body = front_features(body, BOX_W, BOX_H)
    # turn it round so the ring faces the housing
    body = body.rotate((0, 0, 0), (0, 0, 1), 180).translate(PANEL_POS)
    return body


def make_frame():
    cxp, cyp, zb = FR_POS
    # local: front (-Y) face at Y=0, depth towards +Y, centred on X/Z
    outer = (cq.Workplane("XZ").rect(FR_W, FR_H).extrude(-FR_D)
             .edges("|Y").fillet(FR_R)
             .faces("<Y").edges().fillet(FR_FRONT_R))
    inner = (cq.Workplane("XZ", origin=(0, -1, 0))
             .rect(FR_W - 2 * FR_BAR, FR_H - 2 * FR_BAR).extrude(-FR_D - 2)
             .edges("|Y").fillet(FR_R - FR_BAR))
    ring = outer.cut(inner)
    # narrow lip on the back half of the opening
    lip_o = (cq.Workplane("XZ", origin=(0, FR_D - FR_LIP_D, 0))
             .rect(FR_W - 2 * FR_BAR + 0.4, FR_H - 2 * FR_BAR + 0.4).extrude(-FR_LIP_D))
    lip_i = (cq.Workplane("XZ", origin=(0, FR_D - FR_LIP_D - 1, 0))
             .rect(FR_W - 2 * FR_BAR - 2 * FR_LIP, FR_H - 2 * FR_BAR - 2 * FR_LIP)
             .extrude(-FR_LIP_D - 2))
    fr = ring.union(lip_o.cut(lip_i))
    return fr.translate((cxp, cyp - FR_D / 2.0, zb + FR_H / 2.0))


def make_lid():
    cxp, cyp, zb = LID_POS
    lid = (cq.Workplane("XZ").rect(LID_W, LID_H).extrude(-LID_T)
           .edges("|Y").fillet(BOX_R))
    lid = lid.faces("<Y").edges().fillet(LID_EDGE_R)
    lid = lid.faces(">Y").edges().fillet(LID_EDGE_R)
    sq = (cq.Workplane("XZ", origin=(0, 0.3, 0))
          .center(0, LID_SQ_Z - LID_H / 2.0).rect(LID_SQ, LID_SQ).extrude(1.0))
    lid = lid.cut(sq)
    return lid.translate((cxp, cyp - LID_T / 2.0, zb + LID_H / 2.0))


def make_tray():
    x0, cyp, zb = TR_POS
    base = y_box(0, TR_L, -TR_BASE_W / 2, TR_BASE_W / 2, TR_BASE_Z, TR_BASE_Z + TR_BASE_T)
    slot_x0 = TR_STOP_T + TR_SLOT_GAP
    slots = (cq.Workplane("XY")
             .pushPoints([((slot_x0 + TR_L) / 2.0, TR_SLOT_Y),
                          ((slot_x0 + TR_L) / 2.0, -TR_SLOT_Y)])
             .rect(TR_L - slot_x0, TR_SLOT_W).extrude(TR_BASE_T + 2)
             .translate((0, 0, TR_BASE_Z - 1)))
    base = base.cut(slots)
    plate = y_box(TR_L - TR_PLATE_T, TR_L, -TR_W / 2, TR_W / 2, 0, TR_PLATE_H)
    win = y_box(TR_L - TR_PLATE_T - 1, TR_L + 1, -TR_WIN_W / 2, TR_WIN_W / 2,
                TR_WIN_Z0, TR_WIN_Z1)
    plate = plate.cut(win)
    stop = y_box(0, TR_STOP_T, -TR_W / 2, TR_W / 2, 0, TR_STOP_H)
    tr = base.union(plate).union(stop)
    return tr.translate((x0, cyp, zb))


box = make_box()
panel = make_panel()
frame = make_frame()
lid = make_lid()
tray = make_tray()

parts = []
for body in (box, panel, frame, lid, tray):
    parts.extend(body.solids().vals())
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(parts)])

VIEW = {"azimuth": 45, "elevation": 26}
